import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 20.0                 # body diameter
R = D / 2.0
L_TOT = 14.7 * D         # overall length, flange bottom to nose tip
NOSE_L = 1.63 * D        # ogive nose length

# tail (bottom) detail, depths measured down from the end of the body cylinder
TAIL_H = 0.48 * D        # total height of the tail piece below the body cylinder
BOWL_MID_R = 0.87 * R    # convex boat-tail arc from the body end down to the neck
BOWL_MID_Z = 0.16 * D
NECK_R = 0.64 * R        # neck radius
NECK_Z = 0.33 * D
FLARE_MID_R = 0.77 * R   # concave flare from the neck out to the base rim
FLARE_MID_Z = 0.405 * D
FLANGE_R = 0.815 * R     # base rim radius
FLANGE_TOP = 0.455 * D   # depth of the top of the thin rim cylinder
CAV_R = 0.70 * R         # nozzle exit cavity: mouth radius at the base
CAV_TOP_R = 0.25 * R     # ... radius at the top of the conical cavity
CAV_DEPTH = 0.35 * D     # ... depth of the cavity

# fins (4 off, at 0/90/180/270 deg)
FIN_TIP_R = 1.045 * D    # fin tip distance from axis
FIN_LE_ROOT = 2.07 * D   # distance below tip where leading edge meets body
FIN_TIP_TOP = 3.15 * D
FIN_TIP_BOT = 4.24 * D
FIN_TE_ROOT = 5.33 * D
FIN_T = 0.091 * D        # fin thickness
FIN_BEVEL = 0.125 * D    # bevel width on the fin faces
FIN_LE_LAND = 0.018 * D  # narrow flat land left on the leading edge
FIN_ROOT_R = 0.70 * R    # fin root buried inside the body
N_FINS = 4
SEAM_ANGLE = 180.0       # angular position of the revolve seam (cosmetic only)

# ---------------- body of revolution ----------------
z_body_end = TAIL_H
z_nose = L_TOT - NOSE_L

# tangent ogive (radius rho), drawn as a spline through a few points of the arc
rho = (R * R + NOSE_L * NOSE_L) / (2.0 * R)
N_OGIVE_PTS = 6


def ogive_r(dz):
    """radius of the tangent ogive at height dz above the nose base"""
    return math.sqrt(max(rho * rho - dz * dz, 0.0)) + R - rho


ogive_pts = [(ogive_r(NOSE_L * i / N_OGIVE_PTS), z_nose + NOSE_L * i / N_OGIVE_PTS)
             for i in range(1, N_OGIVE_PTS)] + [(0.0, L_TOT)]

prof = (
    cq.Workplane("XZ")
    .moveTo(0, CAV_DEPTH)
    .lineTo(CAV_TOP_R, CAV_DEPTH)
    .lineTo(CAV_R, 0)
    .lineTo(FLANGE_R, 0)
    .lineTo(FLANGE_R, z_body_end - FLANGE_TOP)
    .threePointArc((FLARE_MID_R, z_body_end - FLARE_MID_Z), (NECK_R, z_body_end - NECK_Z))
    .threePointArc((BOWL_MID_R, z_body_end - BOWL_MID_Z), (R, z_body_end))
    .lineTo(R, z_nose)
    .spline(ogive_pts, tangents=[(0, 1), (-NOSE_L, rho - R)], includeCurrent=True)
    .close()
)
# revolve about Z, then turn the body so its (cosmetic) seam sits under the -X fin
body = prof.revolve(360, (0, 0, 0), (0, 1, 0)).rotate((0, 0, 0), (0, 0, 1), SEAM_ANGLE)


# ---------------- fins ----------------
def inset_edges(pts, ds):
    """Offset each edge i (pts[i] -> pts[i+1]) of a CCW convex polygon inward by ds[i]."""
    n = len(pts)
    lines = []
    for i in range(n):
        x1, y1 = pts[i]
        x2, y2 = pts[(i + 1) % n]
        ex, ey = x2 - x1, y2 - y1
        L = math.hypot(ex, ey)
        nx, ny = -ey / L, ex / L          # inward normal for CCW polygon
        lines.append(((x1 + nx * ds[i], y1 + ny * ds[i]), (ex, ey)))
    out = []
    for i in range(n):
        (p1, d1) = lines[i - 1]
        (p2, d2) = lines[i]
        den = d1[0] * d2[1] - d1[1] * d2[0]
        t = ((p2[0] - p1[0]) * d2[1] - (p2[1] - p1[1]) * d2[0]) / den
        out.append((p1[0] + d1[0] * t, p1[1] + d1[1] * t))
    return out


z_le = L_TOT - FIN_LE_ROOT
z_tt = L_TOT - FIN_TIP_TOP
z_tb = L_TOT - FIN_TIP_BOT
z_te = L_TOT - FIN_TE_ROOT
le_slope = (z_le - z_tt) / (FIN_TIP_R - R)
te_slope = (z_tb - z_te) / (FIN_TIP_R - R)
z_le_in = z_le + (R - FIN_ROOT_R) * le_slope
z_te_in = z_te - (R - FIN_ROOT_R) * te_slope

# fin planform in (r, z), counter-clockwise; root edge buried in the body
fin_pts = [
    (FIN_ROOT_R, z_te_in),   # edge 0: trailing edge
    (FIN_TIP_R, z_tb),       # edge 1: tip chord
    (FIN_TIP_R, z_tt),       # edge 2: leading edge
    (FIN_ROOT_R, z_le_in),   # edge 3: root (inside body)
]
half_t = FIN_T / 2.0
half_land = FIN_LE_LAND / 2.0
le_flat = FIN_BEVEL * half_land / half_t        # LE set-back giving the land width
knife_at_land = FIN_BEVEL * half_land / half_t  # knife-edge bevel inset at |y| = half_land
# push the sharp (virtual) leading edge out so the land lands on the nominal LE line
fin_pts = inset_edges(fin_pts, [0.0, 0.0, -le_flat, 0.0])

# sections across the thickness (y): bevel boundary, land edge, mid-plane
sec_face = inset_edges(fin_pts, [FIN_BEVEL, FIN_BEVEL, FIN_BEVEL, 0.0])
sec_land = inset_edges(fin_pts, [knife_at_land, knife_at_land, le_flat, 0.0])
sec_mid = inset_edges(fin_pts, [0.0, 0.0, le_flat, 0.0])


def wire_at(pts, y):
    vs = [cq.Vector(r, y, z) for (r, z) in pts]
    return cq.Wire.makePolygon(vs, close=True)


fin_wires = [
    wire_at(sec_face, -half_t),
    wire_at(sec_land, -half_land),
    wire_at(sec_mid, 0.0),
    wire_at(sec_land, half_land),
    wire_at(sec_face, half_t),
]
fin_solid = cq.Solid.makeLoft(fin_wires, True)
fin = cq.Workplane("XY").add(fin_solid)

result = body
for i in range(N_FINS):
    result = result.union(fin.rotate((0, 0, 0), (0, 0, 1), 90.0 * i))

VIEW = {"azimuth": 45, "elevation": 26}
